import math
import cadquery as cq
from OCP.Geom import Geom_BSplineCurve
from OCP.TColgp import TColgp_Array1OfPnt
from OCP.TColStd import TColStd_Array1OfReal, TColStd_Array1OfInteger
from OCP.gp import gp_Pnt
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.BRep import BRep_Tool

# ---------------- driving dimensions (mm) ----------------
W = 150.0          # outer flange width (X)
L = 184.0          # outer flange length (Y)
R_OUT = 20.0       # plan corner radius of the flange outline
H_FL = 37.0        # flange top height
Z_BAND = 27.5      # bottom of the upper (bulged) band
BAND_IN = 2.5      # inset of the band bottom / top of lower wall
BOT_IN = 10.0      # inset of the bottom edge

# sealing tongue on the flange (insets from flange edge)
TONGUE_H = 2.2
TONGUE_BASE_O, TONGUE_TOP_O = 2.8, 4.9
TONGUE_TOP_I, TONGUE_BASE_I = 5.5, 8.0

# inner cavity
RIM_IN = 8.85      # cavity opening inset at flange level
FLOOR = 4.5        # floor thickness
CAV_R = 13.0       # plan corner radius of the cavity
Z_KNEE = 19.5      # inner wall: near-vertical above, flaring into the floor below
CAV_LOW = ((16.9, FLOOR), (14.77, FLOOR + 0.57), (13.41, FLOOR + 2.31), (11.92, 10.5),
           (10.45, 15.0), (9.15, Z_KNEE))   # (inset, z): floor blend + flared wall
CAV_UP = ((9.15, Z_KNEE), (RIM_IN, H_FL), (RIM_IN - 0.05, H_FL + 4.0))

# mounting tabs
TAB_T = 5.0        # tab thickness (Y)
TAB_OUT = 9.7      # tab projection beyond flange edge
TAB_Z1 = 15.5      # z where tab outer edge starts to slope inward
TAB_YS = (-68.6, -45.0, 45.0, 68.6)
TAB_HOLE_D = 3.0
TAB_R = 1.3        # rounding of the tab tip
TAB_ROOT_R = 2.0   # blend between tab and lower wall
TAB_XB, TAB_ZB = 65.5, 1.5   # where the sloped tab underside meets the wall
TAB_HOLE_X = 5.6   # hole centre outward from flange edge
TAB_HOLE_Z = 18.4

# louvred vents in the front (-Y) wall
VENT_ZS = (21.8, 17.3, 12.8)
VENT_H = 3.0
VENT_ANGLE = 25.0  # slots rise toward the inside (rain shedding)
VENT_R = 0.8       # slot corner radius
VENT_GROUPS = ((-23.2, -1.2), (17.7, 35.9))

# internal vent housing
BLK_X0, BLK_X1, BLK_X2, BLK_X3 = -38.0, 15.7, 25.5, 40.2
BLK_Y0 = -66.0     # inner face of the vent housing
BLK_TOPD = 11.0    # depth of the flat top of the tall housing
BLK_CH_IN = 10.4   # inset where the rear chamfer reaches flange level
BLK_TOP = 42.8     # top of tall housing
BLK_LOW = 34.0     # top of low housing
BLK_WALL = 2.0
POCKET_Z0 = 8.0
POCKETS = ((-35.5, -0.2, 32.5), (17.2, 38.2, 32.0))   # (x0, x1, top z) of the two sensor pockets
POCKET_BACK_IN = 11.0   # inset of the pocket back wall (vents open into it)

# small oval boss on the floor
OVAL_X, OVAL_Y = -18.0, -14.8
OVAL_A, OVAL_B = 11.5, 7.8     # outer size
OVAL_IA, OVAL_IB = 7.2, 3.0    # inner size
OVAL_H = 1.1

# engraved label on +X side (on a flat panel between the inner tabs)
PANEL_IN = 1.8     # panel face inset from flange edge
PANEL_Z0 = 10.0    # bottom of the panel
LABEL = "sensenet + smart cville"
LABEL_SIZE = 7.0
LABEL_Z = 22.3
LABEL_DEPTH = 0.7

# ---------------- helpers ----------------
_WC = (math.sqrt(2) / 2) / (2 - math.sqrt(2) / 2)   # rational weight -> exact 90deg arcs
_K = 1 + _WC


# seam (curve origin) location of the closed B-spline outlines: (side, coordinate)
# side 2 = -X side (coordinate = y), side 3 = -Y side (coordinate = x)
SEAM_TAB = (2, -45.0)   # hidden under a mounting tab on the -X side
SEAM_BLK = (3, 10.0)    # hidden behind the vent housing on the -Y side


def rrect_wire(inset, z, seam=SEAM_TAB, r=None):
    """Rounded rectangle (flange outline offset inward by `inset`, corner radius r
    or the true offset radius) at height z, as a single exact periodic rational
    quadratic B-spline edge (90 deg arcs are exact, no tangent seams)."""
    w, l = W - 2 * inset, L - 2 * inset
    r = R_OUT - inset if r is None else r
    hx, hy, d = w / 2, l / 2, _K * r
    corners = [(hx, -hy), (hx, hy), (-hx, hy), (-hx, -hy)]
    dirs = [(0, 1), (-1, 0), (0, -1), (1, 0)]          # travel direction of side k
    A, C, B = [], [], []
    for k in range(4):
        cx, cy = corners[k]
        din, dout = dirs[k - 1], dirs[k]
        A.append((cx - d * din[0], cy - d * din[1]))
        C.append((cx, cy))
        B.append((cx + d * dout[0], cy + d * dout[1]))
    side, coord = seam
    nxt = (side + 1) % 4
    a = A[nxt]
    p = (corners[side][0], coord) if side in (0, 2) else (coord, corners[side][1])
    m = (2 * p[0] - a[0], 2 * p[1] - a[1])             # extra pole: seam at p
    poles, wts = [m], [1.0]
    for j in range(4):
        k = (nxt + j) % 4
        poles += [A[k], C[k], B[k]]
        wts += [1.0, _WC, 1.0]
    n = len(poles)
    P = TColgp_Array1OfPnt(1, n)
    Wt = TColStd_Array1OfReal(1, n)
    for i, (pp, wt) in enumerate(zip(poles, wts)):
        P.SetValue(i + 1, gp_Pnt(pp[0], pp[1], z))
        Wt.SetValue(i + 1, float(wt))
    kn = TColStd_Array1OfReal(1, n + 1)
    mu = TColStd_Array1OfInteger(1, n + 1)
    for i in range(n + 1):
        kn.SetValue(i + 1, float(i))
        mu.SetValue(i + 1, 1)
    crv = Geom_BSplineCurve(P, Wt, kn, mu, 2, True)
    return cq.Wire.assembleEdges([cq.Edge(BRepBuilderAPI_MakeEdge(crv).Edge())])


def _refine(solid, nv):
    """insert extra knots along the loft direction (geometry unchanged) so the
    smooth walls tessellate finely"""
    for f in solid.Faces():
        srf = BRep_Tool.Surface_s(f.wrapped)
        if srf.DynamicType().Name() != "Geom_BSplineSurface":
            continue
        vk = [srf.VKnot(i) for i in range(1, srf.NbVKnots() + 1)]
        for a, b in zip(vk[:-1], vk[1:]):
            for k in range(1, nv):
                srf.InsertVKnot(a + (b - a) * k / nv, 1, 1e-9, True)
    return solid


def loft(sections, ruled=False, seam=SEAM_TAB, nv=1, r=None):
    s = cq.Solid.makeLoft([rrect_wire(i, z, seam, r) for (i, z) in sections], ruled)
    return _refine(s, nv) if nv > 1 else s


# ---------------- outer body ----------------
# lower wall: circular-arc profile, vertical at the band, curving in to the base
RC = ((BOT_IN - BAND_IN) ** 2 + Z_BAND ** 2) / (2 * (BOT_IN - BAND_IN))


def lower_inset(z):
    return BAND_IN + RC - math.sqrt(RC * RC - (Z_BAND - z) ** 2)


# upper band: convex arc from flange edge down to the band bottom
RB = (BAND_IN ** 2 + (H_FL - Z_BAND) ** 2) / (2 * BAND_IN)


def band_inset(z):
    return RB - math.sqrt(RB * RB - (H_FL - z) ** 2)


lower = loft([(lower_inset(z), z) for z in (0.0, 9.0, 18.0, Z_BAND)], nv=6)
band = loft([(band_inset(z), z) for z in (Z_BAND, 0.5 * (Z_BAND + H_FL), H_FL)], nv=6)
body = cq.Workplane("XY").add(lower.fuse(band))

# sealing tongue (chamfered ridge) on the flange
t_out = loft([(TONGUE_BASE_O, H_FL), (TONGUE_TOP_O, H_FL + TONGUE_H)], ruled=True)
sl = (TONGUE_BASE_I - TONGUE_TOP_I) / TONGUE_H
t_in = loft([(TONGUE_BASE_I + 0.2 * sl, H_FL - 0.2),
             (TONGUE_TOP_I - 0.2 * sl, H_FL + TONGUE_H + 0.2)], ruled=True)
tongue = t_out.cut(t_in)
body = body.union(cq.Workplane("XY").add(tongue), clean=False)

# ---------------- mounting tabs ----------------
xe = W / 2


def make_tab(y, side):
    t = (cq.Workplane("XZ")
         .polyline([(58.0, H_FL), (xe + TAB_OUT, H_FL), (xe + TAB_OUT, TAB_Z1),
                    (TAB_XB, TAB_ZB), (58.0, TAB_ZB)]).close()
         .extrude(TAB_T / 2, both=True))
    sol = t.val()
    # round the free end of the tab (tip edges, top corner and the knee)
    sel = []
    for e in sol.Edges():
        c = e.Center()
        if c.x < 62.0 or c.z < TAB_ZB + 0.3:
            continue
        if c.z > H_FL - 0.1 and abs(e.tangentAt(0.5).x) > 0.9:
            continue
        sel.append(e)
    sol = sol.fillet(TAB_R, sel)
    t = cq.Workplane("XY").add(sol).translate((0, y, 0))
    if side < 0:
        t = t.mirror("YZ")
    return t


for s in (1, -1):
    for y in TAB_YS:
        body = body.union(make_tab(y, s), clean=False)

# flat label panels on the +/-X walls between the two inner tabs
for s in (1, -1):
    yp = abs(TAB_YS[1]) - TAB_T / 2
    pan = (cq.Workplane("XZ")
           .polyline([(60.0, Z_BAND), (xe - PANEL_IN, Z_BAND), (xe - PANEL_IN, PANEL_Z0 + 4.0),
                      (xe - lower_inset(PANEL_Z0) - 0.3, PANEL_Z0), (60.0, PANEL_Z0)]).close()
           .extrude(yp, both=True))
    if s < 0:
        pan = pan.mirror("YZ")
    body = body.union(pan, clean=False)

# blend the tabs into the curved lower wall
_sol = body.val()
_root = []
for e in _sol.Edges():
    c = e.Center()
    if not (60.0 < abs(c.x) < 76.0) or c.z < 1.0 or c.z > Z_BAND:
        continue
    if e.geomType() == "LINE" or e.Length() < 15.0:
        continue
    if any(abs(c.y - (y + sy * TAB_T / 2)) < 0.05 for y in TAB_YS for sy in (-1, 1)):
        _root.append(e)
try:
    _f = _sol.fillet(TAB_ROOT_R, _root)
    if _f.isValid():
        body = cq.Workplane("XY").add(_f)
except Exception:
    pass

# ---------------- inner cavity ----------------
cavity = loft(CAV_LOW, seam=SEAM_BLK, nv=2, r=CAV_R).fuse(
    loft(CAV_UP, ruled=True, seam=SEAM_BLK, r=CAV_R))
body = body.cut(cq.Workplane("XY").add(cavity), clean=False)

# ---------------- vent housing block (inside, against the front wall) ----------------
yb = -L / 2 + TONGUE_BASE_I            # back of housing (merges into the flange)
ych = BLK_Y0 - BLK_TOPD                 # start of the top chamfer
ycl = -L / 2 + BLK_CH_IN                # chamfer lands on flange level here
yfl = -L / 2 + 13.0                     # back edge at floor level (inside the wall)
tall = (cq.Workplane("YZ").workplane(offset=BLK_X0)
        .polyline([(BLK_Y0, FLOOR - 0.5), (BLK_Y0, BLK_TOP), (ych, BLK_TOP),
                   (ycl, H_FL), (yb, H_FL), (yb, 6.0), (yfl, FLOOR - 0.5)])
        .close().extrude(BLK_X2 - BLK_X0))
# sloped step down from the tall housing to the low one
wedge = (cq.Workplane("XZ")
         .polyline([(BLK_X1, BLK_TOP + 1), (BLK_X1, BLK_TOP), (BLK_X2, BLK_LOW),
                    (BLK_X2 + 1, BLK_LOW), (BLK_X2 + 1, BLK_TOP + 1)]).close()
         .extrude(-40).translate((0, -L / 2 - 5, 0)))
tall = tall.cut(wedge, clean=False)
low = (cq.Workplane("YZ").workplane(offset=BLK_X1)
       .polyline([(BLK_Y0, FLOOR - 0.5), (BLK_Y0, BLK_LOW), (yb, BLK_LOW), (yb, 6.0),
                  (yfl, FLOOR - 0.5)])
       .close().extrude(BLK_X3 - BLK_X1))
blk = tall.union(low, clean=False)
body = body.union(blk, clean=False)

# pockets (open toward the interior) behind the two vent groups
pk_depth = BLK_Y0 - (-L / 2 + POCKET_BACK_IN)
for (px0, px1, pz1) in POCKETS:
    pk = (cq.Workplane("XY")
          .box(px1 - px0, pk_depth, pz1 - POCKET_Z0, centered=False)
          .translate((px0, BLK_Y0 - pk_depth + 0.01, POCKET_Z0)))
    body = body.cut(pk, clean=False)

# ---------------- louvred vent slots ----------------
ca, sa = math.cos(math.radians(VENT_ANGLE)), math.sin(math.radians(VENT_ANGLE))
for (xa0, xa1) in VENT_GROUPS:
    for z in VENT_ZS:
        y0 = -L / 2 - 2.0
        ys = -L / 2 + lower_inset(z)          # slot centre on the outer surface
        z0 = z - (ys - y0) * sa / ca
        pl = cq.Plane(origin=((xa0 + xa1) / 2, y0, z0), xDir=(1, 0, 0), normal=(0, ca, sa))
        slot = (cq.Workplane(pl).sketch().rect(xa1 - xa0, VENT_H).vertices().fillet(VENT_R)
                .finalize().extrude(16.0))
        body = body.cut(slot, clean=False)

# ---------------- tab holes (along Y, through all four tabs of a side) ----------------
for s in (1, -1):
    hole = (cq.Workplane("XZ").workplane(offset=-L / 2 - 5)
            .center(s * (xe + TAB_HOLE_X), TAB_HOLE_Z)
            .circle(TAB_HOLE_D / 2).extrude(L + 10))
    body = body.cut(hole, clean=False)

# ---------------- small oval ring on the floor ----------------
ring = (cq.Workplane("XY").workplane(offset=FLOOR - 0.5)
        .center(OVAL_X, OVAL_Y).ellipse(OVAL_A / 2, OVAL_B / 2)
        .extrude(0.5 + OVAL_H))
ring = ring.cut(cq.Workplane("XY").workplane(offset=FLOOR - 1.0)
                .center(OVAL_X, OVAL_Y).ellipse(OVAL_IA / 2, OVAL_IB / 2)
                .extrude(OVAL_H + 2.0))
ring = ring.faces(">Z").edges().fillet(OVAL_H * 0.8)
body = body.union(ring, clean=False)

# ---------------- engraved label on the +X wall ----------------
try:
    x_out = W / 2 - PANEL_IN + 1.5
    label = (cq.Workplane("YZ").workplane(offset=x_out)
             .center(0, LABEL_Z)
             .text(LABEL, LABEL_SIZE, -(1.5 + LABEL_DEPTH + 0.4),
                   font="DejaVu Sans", kind="regular", combine=False))
    body = body.cut(label, clean=False)
except Exception:
    pass

result = body
